import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
N_TEETH = 27            # number of teeth
MODULE = 2.0            # gear module
ADDENDUM = 1.0 * MODULE
DEDENDUM = 1.25 * MODULE
# tooth form: each flank is one circular arc through a root, a pitch and a tip point
TIP_HALF_ANG = 1.70     # deg, angular half-width of a tooth at the tip circle
ROOT_HALF_ANG = 5.00    # deg, angular half-width of a tooth at the root circle
PITCH_HALF_ANG = 180.0 / (2 * N_TEETH)  # deg, half tooth thickness on the pitch circle
TOOTH_PHASE = 0.3       # deg, angular position of tooth 0 measured from +Y toward +Z

DISK_DIA = 50.0         # plain back flange diameter (just above root dia)
DISK_T = 4.0            # back flange thickness
GEAR_T = 4.0            # toothed face width
HUB_DIA = 16.0          # hub diameter
HUB_L = 8.0             # hub length
BORE_DIA = 6.6          # through bore
SET_SCREW_DIA = 3.4     # radial set screw hole in hub (on the -Y side)
SET_SCREW_Z = 0.45      # small vertical offset of the set screw axis
SET_SCREW_OVERDRILL = 0.5  # drill runs this far into the opposite bore wall

# ---------------- derived ----------------
r_pitch = MODULE * N_TEETH / 2.0
r_tip = r_pitch + ADDENDUM
r_root = r_pitch - DEDENDUM
pitch_ang = 2 * math.pi / N_TEETH
th_tip = math.radians(TIP_HALF_ANG)
th_root = math.radians(ROOT_HALF_ANG)
th_pitch = math.radians(PITCH_HALF_ANG)
phase = math.radians(TOOTH_PHASE)


def pol(r, t):
    return (r * math.cos(t), r * math.sin(t))


def gear_profile(wp):
    """closed outline of the toothed section: root arcs, arc flanks, tip arcs.
    Local x of the workplane (+Y in model space) is the direction of tooth 0."""
    wp = wp.moveTo(*pol(r_root, phase - th_root))
    for i in range(N_TEETH):
        c = i * pitch_ang + phase
        wp = wp.threePointArc(pol(r_pitch, c - th_pitch), pol(r_tip, c - th_tip))  # flank
        wp = wp.threePointArc(pol(r_tip, c), pol(r_tip, c + th_tip))   # tip land
        wp = wp.threePointArc(pol(r_pitch, c + th_pitch), pol(r_root, c + th_root))  # flank
        wp = wp.threePointArc(pol(r_root, c + pitch_ang / 2),          # root land
                              pol(r_root, c + pitch_ang - th_root))
    return wp.close()


# gear axis along +X; back flange x=0..DISK_T, teeth next, hub in front
def axial_plane(x0, seam_dir=(0, -1, 0)):
    """plane normal to the gear axis (+X); local x (= cylinder seam side) along seam_dir"""
    return cq.Plane(origin=(x0, 0, 0), xDir=seam_dir, normal=(1, 0, 0))


disk = cq.Workplane(axial_plane(0.0, (0, 0, -1))).circle(DISK_DIA / 2).extrude(DISK_T)
teeth = gear_profile(cq.Workplane("YZ", origin=(DISK_T, 0, 0))).extrude(GEAR_T)
hub = (cq.Workplane(axial_plane(DISK_T + GEAR_T, (0, 1, 0)))
       .circle(HUB_DIA / 2).extrude(HUB_L))

body = disk.union(teeth).union(hub)

total_len = DISK_T + GEAR_T + HUB_L
bore = cq.Workplane(axial_plane(-1.0)).circle(BORE_DIA / 2).extrude(total_len + 2.0)
body = body.cut(bore)

# radial set-screw hole: enters the hub from -Y, crosses the bore and runs
# a little way into the opposite wall (blind there)
x_ss = DISK_T + GEAR_T + HUB_L / 2
ss_start = -HUB_DIA / 2 - 1.0
ss_end = BORE_DIA / 2 + SET_SCREW_OVERDRILL
ss_plane = cq.Plane(origin=(x_ss, ss_start, SET_SCREW_Z), xDir=(1, 0, 0), normal=(0, 1, 0))
set_screw = cq.Workplane(ss_plane).circle(SET_SCREW_DIA / 2).extrude(ss_end - ss_start)
body = body.cut(set_screw)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
